import math
import cadquery as cq

# ---------------------------------------------------------------
# C-shaped snap clip.
# The horseshoe profile (ring + long upper hook + short lower arm +
# neck) lies in the YZ plane and is extruded along X over the full
# thickness.  The neck ends in a flat bottom with rounded corners.
#   * +X half (thickness T_PLUS): carries the stadium shaped foot below
#     the neck and the full-length upper hook.
#   * -X half (thickness T_MINUS): no foot, and the upper hook ends
#     early in a rounded cap.
# Like the original, the ring is split on the plane Z = Z_SEAM into an
# upper and a lower piece (visible as a seam line around the ring).
# ---------------------------------------------------------------

T_PLUS = 7.6            # thickness of the +X half (with foot and long hook)
T_MINUS = 7.2           # thickness of the -X half
Z_SEAM = -0.27          # split plane between upper and lower piece

# neck bottom (end of the flanks) and its rounded corners
Z_NECK = -25.25
FLANK_R_Y = 6.70                 # right flank is vertical at its bottom
FLANK_L_PT = (-9.30, -24.15)     # point on the straight end of the left flank
FLANK_L_DIR = (0.469, -0.883)    # its direction (downwards)
NECK_R_RIGHT = 1.3      # corner radius where the right flank ends
NECK_R_LEFT = 1.6       # corner radius where the left flank ends
NECK_EDGE_R = 1.4       # rounding of the -X bottom edge of the neck
NECK_EDGE_EPS = 0.1     # keeps the rounding tool off the flank surfaces

# foot: stadium below the neck, only on the +X half
FOOT_R = 3.0            # radius of the rounded foot sides
FOOT_CZ = -28.09        # Z of the side-arc centres (bottom at FOOT_CZ - FOOT_R)
FOOT_CL = -6.59         # Y of the left arc centre
FOOT_CR = 4.27          # Y of the right arc centre

# -X half: shortened upper hook with a rounded end
CAP_CENTER = (3.45, 18.95)   # centre of the rounded end (Y, Z)
CAP_R = 3.25                 # radius of that rounded end (~half hook width)
CAP_DIR = (-0.849, 0.529)    # hook direction at the cap (towards the tip)
HOOK_CUT_LEN = 30.0          # extent of the hook removal beyond the cap

# Smooth outline (Y, Z) from the bottom of the right flank: right flank
# -> outer ring -> top of the upper hook -> hook tip -> hook underside
# -> inner ring -> lower arm top -> lower tip -> lower arm underside ->
# left flank.  Interpolated by one B-spline, closed by the neck bottom.
# right corner: arc centre and the tangent point on the right flank
_crr = (FLANK_R_Y - NECK_R_RIGHT, Z_NECK + NECK_R_RIGHT)
_qr = (FLANK_R_Y, _crr[1])
# left corner: arc tangent to the sloped left flank and to the bottom
_nl = (-FLANK_L_DIR[1], FLANK_L_DIR[0])          # normal into the material
_t = (Z_NECK + NECK_R_LEFT * (1 - _nl[1]) - FLANK_L_PT[1]) / FLANK_L_DIR[1]
_ql = (FLANK_L_PT[0] + _t * FLANK_L_DIR[0], FLANK_L_PT[1] + _t * FLANK_L_DIR[1])
_crl = (_ql[0] + NECK_R_LEFT * _nl[0], _ql[1] + NECK_R_LEFT * _nl[1])

OUTLINE = [
    _qr, (7.58, -21.31), (12.44, -16.83), (17.19, -11.72), (19.39, -5.12),
    (19.54, 1.86), (17.60, 8.56), (13.68, 14.38), (8.76, 19.36),
    (2.66, 22.81), (-3.76, 25.66), (-10.41, 27.83), (-16.29, 27.71),
    (-17.57, 26.66), (-17.68, 25.32), (-16.39, 23.54), (-10.37, 21.48),
    (-3.68, 19.44), (2.31, 15.79), (7.42, 11.02), (10.79, 4.89),
    (11.61, -2.02), (9.92, -8.80), (5.05, -13.56), (-1.81, -14.68),
    (-8.59, -13.00), (-14.69, -9.55), (-20.16, -5.17), (-24.59, 0.24),
    (-26.72, 1.78), (-28.76, 1.34), (-30.43, -0.69), (-30.38, -3.15),
    (-26.60, -7.91), (-21.22, -12.37), (-15.36, -16.22), (-10.71, -21.43),
    _ql,
]

T_TOTAL = T_PLUS + T_MINUS


# ---- main body: profile extruded over the full thickness ------------
def _arc_mid(c, r, p0, p1):
    a0 = math.atan2(p0[1] - c[1], p0[0] - c[0])
    a1 = math.atan2(p1[1] - c[1], p1[0] - c[0])
    da = (a1 - a0 + math.pi) % (2 * math.pi) - math.pi
    am = a0 + da / 2
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


_bl = (_crl[0], Z_NECK)          # bottom tangent point, left corner
_br = (_crr[0], Z_NECK)          # bottom tangent point, right corner
body = (cq.Workplane("YZ").moveTo(*OUTLINE[0])
        .spline(OUTLINE[1:], includeCurrent=True,
                tangents=[(0.0, 1.0), FLANK_L_DIR], scale=False)
        .threePointArc(_arc_mid(_crl, NECK_R_LEFT, _ql, _bl), _bl)
        .lineTo(*_br)
        .threePointArc(_arc_mid(_crr, NECK_R_RIGHT, _br, _qr), _qr)
        .close()
        .extrude(T_TOTAL)
        .translate((-T_MINUS, 0, 0)))

# rounded bottom edge of the neck on the -X face (the rounding circle
# is sunk by NECK_EDGE_EPS so it cuts the faces instead of touching them)
ecx = -T_MINUS + NECK_EDGE_R - NECK_EDGE_EPS
ecz = Z_NECK + NECK_EDGE_R - NECK_EDGE_EPS
edge_cut = (cq.Workplane("XZ")
            .center(ecx - NECK_EDGE_R, ecz - NECK_EDGE_R)
            .rect(2 * NECK_EDGE_R, 2 * NECK_EDGE_R)
            .extrude(30.0, both=True)
            .cut(cq.Workplane("XZ").center(ecx, ecz).circle(NECK_EDGE_R)
                 .extrude(30.0, both=True)))
body = body.cut(edge_cut)

# ---- foot on the +X half ---------------------------------------------
foot = (cq.Workplane("YZ")
        .moveTo(FOOT_CR, FOOT_CZ - FOOT_R)
        .threePointArc((FOOT_CR + FOOT_R, FOOT_CZ),
                       (FOOT_CR, FOOT_CZ + FOOT_R))
        .lineTo(FOOT_CR, Z_NECK + 1.0)
        .lineTo(FOOT_CL, Z_NECK + 1.0)
        .lineTo(FOOT_CL, FOOT_CZ + FOOT_R)
        .threePointArc((FOOT_CL - FOOT_R, FOOT_CZ),
                       (FOOT_CL, FOOT_CZ - FOOT_R))
        .close()
        .extrude(T_PLUS))
body = body.union(foot)

# ---- -X half: shorten the upper hook, ending in a rounded cap -------
cy, cz = CAP_CENTER
ang = math.degrees(math.atan2(CAP_DIR[1], CAP_DIR[0]))
hook_box = (cq.Workplane("XY")
            .box(T_MINUS + 1.0, HOOK_CUT_LEN, 16.0,
                 centered=(False, False, True))
            .rotate((0, 0, 0), (1, 0, 0), ang)
            .translate((-T_MINUS - 1.0, cy, cz)))
cap_cyl = (cq.Workplane("YZ").center(cy, cz).circle(CAP_R)
           .extrude(T_MINUS + 2.0).translate((-T_MINUS - 1.0, 0, 0)))
body = body.cut(hook_box.cut(cap_cyl))

# ---- seam: upper and lower piece joined on Z = Z_SEAM ---------------
# lower piece = everything below the seam plane plus the lower arm tip
lower_region = (cq.Workplane("XY")
                .box(60, 100, 60, centered=(True, True, False))
                .translate((0, 0, Z_SEAM - 60))
                .union(cq.Workplane("XY")
                       .box(60, 40, 20, centered=(True, False, False))
                       .translate((0, -60, -10))))
result = body.cut(lower_region).union(body.intersect(lower_region),
                                      clean=False)

VIEW = {"azimuth": 45, "elevation": 26}
